import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 240.0          # overall length (Y)
W = 60.0           # overall width (X)
H = 24.0           # overall height (Z)
FLOOR_T = 7.2      # floor thickness of the main tray
LEDGE_H = 8.6      # height of the ledge at the +Y end
WALL_T = 4.7       # back wall thickness (-X side)
END_FRONT = 12.0   # length of the full block at the -Y end
END_BACK = 12.0    # length of the +Y end (corner block + ledge)
BLOCK_W = 12.0     # X width of the tall corner block at +Y end

HOLE_X = 4.6       # hole offset from -X face
HOLE_Y = 4.9       # hole offset from -Y face
HOLE_D = 5.0       # hole diameter (tap drill size)
HOLE_DEPTH = 12.0  # blind hole depth
CSK_D = 6.4        # top chamfer / countersink diameter
CSK_ANGLE = 90.0   # countersink included angle

# ---------------- base block ----------------
body = cq.Workplane("XY").box(W, L, H, centered=(True, True, False))

# main tray pocket (open towards +X)
pocket_len = L - END_FRONT - END_BACK
pocket_w = W - WALL_T
pocket = (
    cq.Workplane("XY")
    .box(pocket_w, pocket_len, H - FLOOR_T, centered=False)
    .translate((-W / 2 + WALL_T, -L / 2 + END_FRONT, FLOOR_T))
)
body = body.cut(pocket)

# +Y end: lower ledge next to the tall corner block
ledge_cut = (
    cq.Workplane("XY")
    .box(W - BLOCK_W, END_BACK, H - LEDGE_H, centered=False)
    .translate((-W / 2 + BLOCK_W, L / 2 - END_BACK, LEDGE_H))
)
body = body.cut(ledge_cut)

# chamfered blind hole in the -Y end block
body = (
    body.faces(">Z").workplane(centerOption="ProjectedOrigin", origin=(0, 0, 0))
    .pushPoints([(-W / 2 + HOLE_X, -L / 2 + HOLE_Y)])
    .cskHole(HOLE_D, CSK_D, CSK_ANGLE, depth=HOLE_DEPTH)
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
